import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
# base (stadium shaped flange)
TUBE_PITCH = 30.0          # distance between the two tube axes (X)
BASE_R = 15.0              # end radius of the stadium base
BASE_T = 2.0               # base thickness

# tubes (revolved profile)
CONE_R0 = 12.5             # radius of the short cylindrical foot of the cone
FOOT_TOP = 5.1             # Z where the taper starts
CONE_R1 = 10.9             # cone radius at top
CONE_TOP = 13.1            # Z of cone top
RING_R = 10.15             # ring / cylinder radius
GROOVE_R = 8.75            # groove radius
GROOVE1 = (20.6, 22.05)    # lower groove Z range
GROOVE2 = (25.85, 27.3)    # upper groove Z range
RING_TOP = 30.35           # top of upper ring (outer edge)
CONE2_TOP = 31.05          # shallow cone from the ring up to the lip
LIP_R = 8.5                # thin lip outer radius
TUBE_TOP = 31.95           # top of lip
BORE_R = 7.85              # bore radius
BORE_CH = 0.5              # inner chamfer on the lip of the -X tube only
SEAM_ANGLE = 45.0          # where the revolve seam of the tubes sits (deg about Z)
FLOOR_HOLE_D = 7.0         # two holes in the floor of every tube
FLOOR_HOLE_OFF = 6.15      # their offset along Y from the tube axis

# vertical tab / plate
PLATE_W = 29.7             # overall width (X) incl. round ends
PLATE_Y0 = 12.25           # front face Y
PLATE_Y1 = 16.1            # back face Y
PLATE_H = 73.8             # overall height

# bracket block behind the plate
BR_W = 26.6                # width (X)
BR_Y1 = 24.75              # back face Y
BR_H = 28.4                # height of block top
BR_CORNER_R = 3.0          # rounded back vertical corners
BR_FOOT_INSET = 0.25       # lowest BASE_T of the block is inset by this much
BR_HOLE_D = 6.5            # two vertical through holes
BR_HOLE_X = 5.6
BR_HOLE_Y = 19.55
WIN_W = 7.5                # rectangular windows on the back face
WIN_Y0 = PLATE_Y1          # windows reach in to the plate
WIN_Z0 = 2.05
WIN_Z1 = 24.4

# curved gusset fins on top of the block
FIN_TOP = 38.8             # Z where fins meet the plate
FIN_T = 4.0                # fin thickness (X)
MID_FIN_DEPTH = BR_Y1 - PLATE_Y1       # middle fin reaches back face
OUT_FIN_DEPTH = 5.0                    # outer fins are shorter

# ---------------- base ----------------
base = (
    cq.Workplane("XY")
    .slot2D(TUBE_PITCH + 2 * BASE_R, 2 * BASE_R, 0)
    .extrude(BASE_T)
)

# ---------------- tubes ----------------
def tube_profile(inner_chamfer=False):
    pts = [
        (BORE_R, BASE_T),
        (CONE_R0, BASE_T),
        (CONE_R0, FOOT_TOP),
        (CONE_R1, CONE_TOP),
        (RING_R, CONE_TOP),
        (RING_R, GROOVE1[0]),
        (GROOVE_R, GROOVE1[0]),
        (GROOVE_R, GROOVE1[1]),
        (RING_R, GROOVE1[1]),
        (RING_R, GROOVE2[0]),
        (GROOVE_R, GROOVE2[0]),
        (GROOVE_R, GROOVE2[1]),
        (RING_R, GROOVE2[1]),
        (RING_R, RING_TOP),
        (LIP_R, CONE2_TOP),
        (LIP_R, TUBE_TOP),
    ]
    if inner_chamfer:
        pts += [(LIP_R - 0.15, TUBE_TOP), (BORE_R, TUBE_TOP - BORE_CH)]
    else:
        pts += [(BORE_R, TUBE_TOP)]
    return pts


def make_tube(x, inner_chamfer=False):
    prof = (
        cq.Workplane("XZ")
        .polyline(tube_profile(inner_chamfer))
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )
    # turn the revolve seam to the +X+Y diagonal (least visible) and place it
    prof = prof.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    return prof.translate((x, 0, 0))


part = base
for sx in (-1, 1):
    part = part.union(make_tube(sx * TUBE_PITCH / 2, inner_chamfer=(sx < 0)))

# floor holes (through the base inside each tube)
hole_pts = [
    (sx * TUBE_PITCH / 2, sy * FLOOR_HOLE_OFF) for sx in (-1, 1) for sy in (-1, 1)
]
floor_holes = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints(hole_pts)
    .circle(FLOOR_HOLE_D / 2)
    .extrude(BASE_T + 2)
)
part = part.cut(floor_holes)

# ---------------- plate ----------------
plate_t = PLATE_Y1 - PLATE_Y0
plate = (
    cq.Workplane("XY")
    .center(0, (PLATE_Y0 + PLATE_Y1) / 2)
    .slot2D(PLATE_W, plate_t, 0)
    .extrude(PLATE_H)
)
part = part.union(plate)

# ---------------- bracket block ----------------
def block_body(inset, z0, z1):
    d = BR_Y1 - inset - PLATE_Y1
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .center(0, PLATE_Y1 - 0.5 + (d + 0.5) / 2)
        .rect(BR_W - 2 * inset, d + 0.5)
        .extrude(z1 - z0)
        .edges("|Z and >Y")
        .fillet(BR_CORNER_R - inset)
    )


# main block sits on a slightly smaller foot at the base level
block = block_body(0.0, BASE_T, BR_H).union(block_body(BR_FOOT_INSET, 0.0, BASE_T + 0.01))


def fin(x0, x1, depth):
    """Curved gusset between plate back face and block top, in YZ plane."""
    h = FIN_TOP - BR_H
    # circle with vertical tangent at the block top, passing the plate top point
    R = (depth ** 2 + h ** 2) / (2 * depth)
    cy = PLATE_Y1 + depth - R
    cz = BR_H
    ang0 = 0.0
    ang1 = math.atan2(h, PLATE_Y1 - cy)
    am = 0.5 * (ang0 + ang1)
    mid = (cy + R * math.cos(am), cz + R * math.sin(am))
    yb = PLATE_Y1 - 0.5
    prof = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .moveTo(yb, BR_H - 0.5)
        .lineTo(PLATE_Y1 + depth, BR_H - 0.5)
        .lineTo(PLATE_Y1 + depth, BR_H)
        .threePointArc(mid, (PLATE_Y1, FIN_TOP))
        .lineTo(yb, FIN_TOP)
        .close()
        .extrude(x1 - x0)
    )
    return prof


block = block.union(fin(-FIN_T / 2, FIN_T / 2, MID_FIN_DEPTH))
for s in (-1, 1):
    xa = s * (BR_W / 2 - FIN_T)
    xb = s * BR_W / 2
    block = block.union(fin(min(xa, xb), max(xa, xb), OUT_FIN_DEPTH))

# vertical through holes
br_holes = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints([(-BR_HOLE_X, BR_HOLE_Y), (BR_HOLE_X, BR_HOLE_Y)])
    .circle(BR_HOLE_D / 2)
    .extrude(FIN_TOP + 2)
)
block = block.cut(br_holes)

# windows on the back face
win_d = BR_Y1 - WIN_Y0 + 1.0
windows = (
    cq.Workplane("XY")
    .workplane(offset=WIN_Z0)
    .pushPoints(
        [(-BR_HOLE_X, WIN_Y0 + win_d / 2), (BR_HOLE_X, WIN_Y0 + win_d / 2)]
    )
    .rect(WIN_W, win_d)
    .extrude(WIN_Z1 - WIN_Z0)
)
block = block.cut(windows)

part = part.union(block)

result = part
